import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Driving dimensions (mm)
# ---------------------------------------------------------------------------
L = 160.0          # overall length (X)
D = 25.0           # overall depth (Y, front face at Y=0)
H = 50.0           # overall height (Z)

END_LEN = 33.4     # length of each end block along X
DRAFT = 1.5        # draft angle of the end blocks (deg)
INNER_DRAFT = 2.7  # draft of the end block faces towards the centre (deg)
CORNER_R = 7.2     # big vertical radius at the front/outer corners
FRONT_T = 7.0      # end block front wall thickness
END_T = 6.4        # end wall thickness
NOTCH_X = 3.8      # back notch on the end wall
NOTCH_Y = 21.3

DECK_Z = 34.6      # underside of the top deck / rail
CENTER_Z0 = 4.9    # underside of the central wall
RAIL_Y0 = 1.6      # rail front face
RAIL_Y1 = 12.0     # rail back face
WALL_Y0_TOP = 2.3  # ribbed wall front face at the top
WALL_Y0_BOT = 3.9  # ribbed wall front face at the bottom (draft)
WALL_Y1 = 7.0      # ribbed wall back face

N_GROOVES = 12
GROOVE_PITCH = 6.9
GROOVE_W = 3.45
GROOVE_D_TOP = 1.2
GROOVE_D_BOT = 0.3
GROOVE_Z0 = CENTER_Z0 + 0.8

BOSS_C = (14.7, 11.7)   # hook boss (left end)
BOSS_R = 3.6
PIN_HOLE_D = 4.0
RECT_HOLE = (19.6, 30.6, 7.1, 13.0)   # x0, x1, y0, y1 (left end)
BLOCK_TOP = 16.4
TAB_Y = 13.3       # right end: height of the tab / lobe start
LOBE_X = 138.7     # right end: left face of the lobe

SLOT_W = 5.8
SLOT_X0 = 12.4     # front slot position (from the end)
SLOT_Z1 = 35.0     # top of the slots
SLOT_DEPTH_TOP = 3.6
SLOT_DEPTH_BOT = 1.5
ESLOT_Y0 = 12.0    # end-face slot
ESLOT_Y1 = 17.2
INNER_EDGE_R = 3.0
BOTTOM_R = 2.0
BACK_BOTTOM_R = 4.0

# right-end latch details
BORE_Y = 6.25
BORE_Z = 44.6
BORE_D = 4.2
BORE_CSK_D = 7.7
WIN_X0 = 145.0
CHAN_D = 7.4       # half-pipe channel behind the window
CHAN_END = 1.75    # wall left at the end face (countersunk bore)
WIN_Z0 = BORE_Z - CHAN_D / 2
WIN_Z1 = BORE_Z + CHAN_D / 2
WIN_Y1 = 4.6       # depth of the window opening in the front face
RAMP_X0 = 127.2
RAMP_Z0 = 35.5
RAMP_D = 1.3

DR = math.tan(math.radians(DRAFT))


def face_y(z):
    """Y of the drafted front face of the end blocks at height z."""
    return (H - z) * DR


def halfspace(point, normal, size=400.0):
    """Large box occupying the side of the plane opposite to `normal`."""
    n = cq.Vector(*normal).normalized()
    ref = cq.Vector(1, 0, 0) if abs(n.x) < 0.9 else cq.Vector(0, 1, 0)
    xd = ref.cross(n).normalized()
    pl = cq.Plane(origin=cq.Vector(*point), xDir=xd, normal=n)
    return cq.Workplane(pl).rect(size, size).extrude(-size / 2)


# ---------------------------------------------------------------------------
# End blocks (drafted L-shaped shells)
# ---------------------------------------------------------------------------
def end_block_left():
    blk = (
        cq.Workplane("XY").workplane(offset=H)
        .moveTo(0, CORNER_R)
        .lineTo(0, D)
        .lineTo(END_LEN, D)
        .lineTo(END_LEN, 0)
        .lineTo(CORNER_R, 0)
        .threePointArc(
            (CORNER_R * (1 - math.cos(math.pi / 4)), CORNER_R * (1 - math.sin(math.pi / 4))),
            (0, CORNER_R),
        )
        .close()
        .extrude(-H, taper=DRAFT)
    )
    # steeper draft on the inner side face (towards the centre section)
    ti = math.tan(math.radians(INNER_DRAFT))
    blk = blk.intersect(halfspace((END_LEN, 0, H), (1, 0, -ti)))
    # vertical edge roundings
    blk = blk.edges(cq.selectors.BoxSelector((END_LEN - 4, -0.5, -1), (END_LEN + 1, 1.6, H + 1))).fillet(INNER_EDGE_R)
    blk = blk.edges(cq.selectors.BoxSelector((-0.5, D - 1.5, -1), (1.5, D + 0.5, H + 1))).fillet(0.8)
    # rounded bottom edges
    blk = blk.faces("<Z").edges().fillet(BOTTOM_R)
    # hollow behind the front wall / inside the end wall
    pocket = cq.Workplane("XY").box(60, 30, H + 2, centered=False).translate((END_T, FRONT_T, -1))
    notch = cq.Workplane("XY").box(END_T - NOTCH_X, 10, H + 2, centered=False).translate(
        (NOTCH_X, NOTCH_Y, -1))
    blk = blk.cut(pocket).cut(notch)
    # large rounding of the back-bottom corner of the end wall (drafted back face)
    t = DR
    y0 = D - H * t
    r = BACK_BOTTOM_R
    s = math.sqrt(1 + t * t)
    yc = y0 + t * r - r * s
    yt = yc + r / s
    zt = r - r * t / s
    ang = math.atan2(zt - r, yt - yc) / 2 - math.pi / 4
    mid = (yc + r * math.cos(ang), r + r * math.sin(ang))
    cutter = (
        cq.Workplane("YZ").workplane(offset=-1)
        .moveTo(yc, -1)
        .lineTo(yc, 0)
        .threePointArc(mid, (yt, zt))
        .lineTo(yt + 3, zt)
        .lineTo(yt + 3, -1)
        .close()
        .extrude(END_T + 2)
    )
    blk = blk.cut(cutter)
    return blk


def deck_left():
    """Top deck of the left end: hook boss, latch finger and rectangular block."""
    cx, cy = BOSS_C
    a0 = math.acos((11.6 - cx) / BOSS_R)            # angle where boss meets x=11.6
    p_low = (11.6, cy - BOSS_R * math.sin(a0))
    a1 = math.radians(122.0)
    p_up = (cx + BOSS_R * math.cos(a1), cy + BOSS_R * math.sin(a1))
    mid = (cx - BOSS_R, cy)
    prof = (
        cq.Workplane("XY").workplane(offset=DECK_Z)
        .moveTo(11.6, 5.0)
        .lineTo(*p_low)
        .threePointArc(mid, p_up)
        .spline([(13.3, 16.7), (12.1, 19.9), (11.1, 23.3), (11.5, 24.7)], includeCurrent=True)
        .threePointArc((12.45, 25.0), (13.4, 24.7))
        .spline([(14.9, 23.8), (15.7, 21.8), (16.3, 19.4), (17.5, 17.4), (19.3, 16.55), (20.6, 16.4)],
                includeCurrent=True)
        .lineTo(31.3, BLOCK_TOP)
        .threePointArc((32.15, 16.05), (32.5, 15.2))
        .lineTo(32.5, 13.2)
        .threePointArc((32.85, 12.35), (33.7, RAIL_Y1))
        .lineTo(40.0, RAIL_Y1)
        .lineTo(40.0, 5.0)
        .close()
        .extrude(H - DECK_Z)
    )
    return prof


def build():
    left = end_block_left()
    right = left.mirror("YZ", basePointVector=(L / 2, 0, 0))
    body = left.union(right)

    # central rail (top band)
    rail = cq.Workplane("XY").box(L - 2 * END_LEN + 2, RAIL_Y1 - RAIL_Y0, H - DECK_Z,
                                  centered=False).translate((END_LEN - 1, RAIL_Y0, DECK_Z))
    body = body.union(rail)

    # central ribbed wall (drafted front)
    wall = (
        cq.Workplane("YZ").workplane(offset=END_LEN - 3)
        .polyline([(WALL_Y0_TOP, DECK_Z + 0.5), (WALL_Y0_BOT, CENTER_Z0),
                   (WALL_Y1, CENTER_Z0), (WALL_Y1, DECK_Z + 0.5)])
        .close()
        .extrude(L - 2 * END_LEN + 6)
    )
    body = body.union(wall)

    # top deck features, left and mirrored right
    dl = deck_left()
    dr = dl.mirror("YZ", basePointVector=(L / 2, 0, 0))
    body = body.union(dl).union(dr)

    # right end: rectangular block is open to the back, leaving a tab and a lobe
    rx0 = L - RECT_HOLE[1]
    rx1 = L - RECT_HOLE[0]
    open1 = cq.Workplane("XY").box(rx1 - rx0, TAB_Y - FRONT_T, H, centered=False).translate(
        (rx0, FRONT_T, DECK_Z - 1))
    open2 = cq.Workplane("XY").box(LOBE_X - rx0, 20, H, centered=False).translate((rx0, TAB_Y, DECK_Z - 1))
    open3 = cq.Workplane("XY").box(rx0 - (L - END_LEN) + 0.2, 20, H, centered=False).translate(
        (L - END_LEN - 0.2, TAB_Y, DECK_Z - 1))
    body = body.cut(open1).cut(open2).cut(open3)

    # vertical pin holes in the hook bosses
    for x in (BOSS_C[0], L - BOSS_C[0]):
        hole = cq.Workplane("XY").circle(PIN_HOLE_D / 2).extrude(H).translate((x, BOSS_C[1], DECK_Z - 1))
        body = body.cut(hole)
    # rectangular hole through the left deck
    rh = (cq.Workplane("XY").rect(RECT_HOLE[1] - RECT_HOLE[0], RECT_HOLE[3] - RECT_HOLE[2])
          .extrude(H).edges("|Z").fillet(0.5)
          .translate(((RECT_HOLE[0] + RECT_HOLE[1]) / 2, (RECT_HOLE[2] + RECT_HOLE[3]) / 2, DECK_Z - 1)))
    body = body.cut(rh)

    # grooves on the ribbed wall
    span = (N_GROOVES - 1) * GROOVE_PITCH
    x_start = L / 2 - span / 2 - GROOVE_W / 2
    def wall_y(z):
        return WALL_Y0_TOP + (WALL_Y0_BOT - WALL_Y0_TOP) * (DECK_Z - z) / (DECK_Z - CENTER_Z0)
    gprof = [(WALL_Y0_TOP - 1.0, DECK_Z),
             (WALL_Y0_TOP + GROOVE_D_TOP, DECK_Z),
             (wall_y(GROOVE_Z0) + GROOVE_D_BOT, GROOVE_Z0),
             (WALL_Y0_TOP - 1.0, GROOVE_Z0)]
    grooves = None
    for i in range(N_GROOVES):
        g = (cq.Workplane("YZ").workplane(offset=x_start + i * GROOVE_PITCH)
             .polyline(gprof).close().extrude(GROOVE_W))
        grooves = g if grooves is None else grooves.union(g)
    body = body.cut(grooves)

    # slots on the front faces of the end blocks (tapered depth)
    sprof = [(-2.0, -1.0), (face_y(0) + SLOT_DEPTH_BOT, -1.0),
             (face_y(SLOT_Z1) + SLOT_DEPTH_TOP, SLOT_Z1), (-2.0, SLOT_Z1)]
    for x0 in (SLOT_X0, L - SLOT_X0 - SLOT_W):
        s = cq.Workplane("YZ").workplane(offset=x0).polyline(sprof).close().extrude(SLOT_W)
        body = body.cut(s)
    # slots on the end faces
    eprof = [(-2.0, -1.0), (face_y(0) + SLOT_DEPTH_BOT, -1.0),
             (face_y(SLOT_Z1) + SLOT_DEPTH_TOP, SLOT_Z1), (-2.0, SLOT_Z1)]
    for side in (0, 1):
        s = cq.Workplane("XZ").workplane(offset=-ESLOT_Y0).polyline(eprof).close().extrude(-(ESLOT_Y1 - ESLOT_Y0))
        if side == 1:
            s = s.mirror("YZ", basePointVector=(L / 2, 0, 0))
        body = body.cut(s)

    # right end: lead-in ramp below the latch window.  The ramp plane starts flush on the
    # (drafted) front face at RAMP_Z0 and is RAMP_D deep at the lower corner of the window;
    # it is bounded above by the diagonal running from (RAMP_X0, RAMP_Z0) to that corner.
    y_a = face_y(RAMP_Z0)
    yb = face_y(WIN_Z0) + RAMP_D
    k = (yb - y_a) / (WIN_Z0 - RAMP_Z0)           # ramp plane: Y = y_a + k (Z - RAMP_Z0)
    s = (WIN_Z0 - RAMP_Z0) / (WIN_X0 - RAMP_X0)   # diagonal:   Z = RAMP_Z0 + s (X - RAMP_X0)
    hs_ramp = halfspace((RAMP_X0, y_a, RAMP_Z0), (0, 1, -k))
    hs_diag = halfspace((RAMP_X0, 0, RAMP_Z0), (-s, 0, 1))
    bound = cq.Workplane("XY").box(END_LEN + 4, 12, 20, centered=False).translate(
        (L - END_LEN - 1, -2, RAMP_Z0))
    wedge = bound.intersect(hs_ramp).intersect(hs_diag)
    body = body.cut(wedge)

    # right end: latch window with a half-pipe channel, pin bore with countersink
    win = (cq.Workplane("YZ").workplane(offset=WIN_X0)
           .polyline([(-1.0, WIN_Z0), (WIN_Y1, WIN_Z0), (WIN_Y1, WIN_Z1), (-1.0, WIN_Z1)])
           .close().extrude(L + 2 - WIN_X0))
    body = body.cut(win)
    chan = (cq.Workplane("YZ").workplane(offset=WIN_X0).center(BORE_Y, BORE_Z)
            .circle(CHAN_D / 2).extrude(L - WIN_X0 - CHAN_END))
    body = body.cut(chan)
    bore = cq.Workplane("YZ").workplane(offset=WIN_X0).center(BORE_Y, BORE_Z).circle(BORE_D / 2).extrude(L + 2 - WIN_X0)
    body = body.cut(bore)
    csk_depth = (BORE_CSK_D - BORE_D) / 2
    csk = cq.Solid.makeCone(BORE_D / 2, BORE_CSK_D / 2 + 0.3, csk_depth + 0.3,
                            cq.Vector(L - csk_depth, BORE_Y, BORE_Z), cq.Vector(1, 0, 0))
    body = body.cut(cq.Workplane("XY").add(csk))

    return body


result = build()
